import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Parallel (linkage) gripper: housing made of two T-shaped side plates and a
# box core, two parallelogram linkages and two serrated jaws.
# X = width, Y = depth, Z = up.  Bottom of housing at Z = 0.
# ---------------------------------------------------------------------------

# ---- housing plates -------------------------------------------------------
BODY_HW = 35.2        # half width of lower body
HEAD_HW = 74.1        # half width of head (lobe tips)
LOBE_Z0 = 114.0       # lower edge of the lobes
NECK_R = 25.0         # concave radius between body and lobe
TOP_Z = 159.5         # flat top of head plate
TOP_FLAT_HW = 17.0    # half width of flat top
LOBE_TOP_Z = 145.5    # top edge Z at the lobe tip
LOBE_R_LO = 13.0      # lower corner radius of lobe tip
LOBE_R_HI = 13.0      # upper corner radius of lobe tip
PLATE_T = 4.5         # plate thickness
PLATE_EDGE_R = 0.8    # round on the outer face perimeter
GAP_HW = 16.4         # half of gap between plates (= half depth of core)
OUT_HW = GAP_HW + PLATE_T
CORNER_R = 5.0
SCREW_R = 3.4         # screw head radius
SCREW_H = 0.6         # screw head protrusion

# ---- core -----------------------------------------------------------------
CORE_TOP = 92.0
CORE_TOP_R = 6.0
SIDE_HOLE_R = 1.3
BOTTOM_REC_R = 8.5

# ---- linkage pivots (left side, mirrored to the right) ----------------------
A_O = (-66.3, 130.2)   # plate, outer pivot
A_I = (-49.4, 133.5)   # plate, inner pivot
LINK_V = (37.2, 59.5)  # link vector (parallelogram)
B_O = (A_O[0] + LINK_V[0], A_O[1] + LINK_V[1])   # jaw, outer pivot
B_I = (A_I[0] + LINK_V[0], A_I[1] + LINK_V[1])   # jaw, inner pivot
LINK_R = 5.8           # link end radius (link width = 2R)
OUTER_LINK_HW = 15.3   # half depth of the wide outer link
FORK_HW = 10.3         # half depth of fork gap / jaw knuckle
INNER_FORK_L = 16.0    # fork depth at the jaw end of the inner link
INNER_SLOT_C = 34.0    # slot centre along the inner link
INNER_SLOT_LEN = 32.0
PIVOT_R = 4.8          # pivot pin radius in plates
POCKET_D = 9.5         # depth of window pocket in outer link
SLOT_C = 35.5          # slot centre along the outer link
SLOT_LEN = 31.0
PIN_RECESS = 4.3       # pin end below plate outer face
PIN_BORE_R = 1.5       # hollow pin bore

# ---- jaws --------------------------------------------------------------------
JAW_HW = 13.0
JAW_GAP = 0.15
JAW_Z0 = 206.5
JAW_Z1 = 236.6
JAW_D_HW = 15.0
STEM_HW = 10.5
STEM_Z0 = 180.7
STEM_SIDE_Z = 187.0     # where the arm underside leaves the stem
KNUCKLE_R = 6.5
ARM_SLOPE = 0.27       # rise of jaw arm top edge towards the centre
ARM_NECK_HW = 12.0     # half width of jaw neck under the block
ARM_NECK_R = 7.5       # concave radius between arm top and neck
JAW_TOP_R = 4.0
TEETH_N = 9
TEETH_P = 3.25
TEETH_D = 1.3


def fillet_poly(wp, pts, radii):
    """Closed polygon with per-vertex fillet radii drawn on workplane wp."""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        r = radii[i]
        if r <= 0:
            segs.append((p, None, p))
            continue
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        d1 = (a[0] - p[0], a[1] - p[1])
        d2 = (b[0] - p[0], b[1] - p[1])
        l1 = math.hypot(*d1)
        l2 = math.hypot(*d2)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosphi = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        phi = math.acos(cosphi)
        t = r / math.tan(phi / 2.0)
        t1 = (p[0] + d1[0] * t, p[1] + d1[1] * t)
        t2 = (p[0] + d2[0] * t, p[1] + d2[1] * t)
        bx, by = d1[0] + d2[0], d1[1] + d2[1]
        bl = math.hypot(bx, by)
        bx, by = bx / bl, by / bl
        h = r / math.sin(phi / 2.0)
        c = (p[0] + bx * h, p[1] + by * h)
        m = (c[0] - bx * r, c[1] - by * r)
        segs.append((t1, m, t2))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if m is not None:
            w = w.threePointArc(m, t2)
    return w.close()


def xz_solid(builder, y0, y1):
    """Extrude an XZ profile (local x = X, local y = Z) between Y=y0 and Y=y1."""
    wp = cq.Workplane("XZ", origin=(0, y1, 0))
    return builder(wp).extrude(y1 - y0)


# ---- housing plates ---------------------------------------------------------------
def plate_profile(wp):
    pts = [
        (-BODY_HW, 0.0), (BODY_HW, 0.0),
        (BODY_HW, LOBE_Z0), (HEAD_HW, LOBE_Z0), (HEAD_HW, LOBE_TOP_Z),
        (TOP_FLAT_HW, TOP_Z), (-TOP_FLAT_HW, TOP_Z),
        (-HEAD_HW, LOBE_TOP_Z), (-HEAD_HW, LOBE_Z0), (-BODY_HW, LOBE_Z0),
    ]
    radii = [CORNER_R, CORNER_R, NECK_R, LOBE_R_LO, LOBE_R_HI, 6.0, 6.0, LOBE_R_HI, LOBE_R_LO, NECK_R]
    return fillet_poly(wp, pts, radii)


SCREWS = [(-13.0, 155.0), (13.0, 155.0), (-29.5, 86.4), (29.5, 86.4),
          (-29.8, 5.2), (29.8, 5.2)]
PIVOTS = [A_O, A_I, (-A_O[0], A_O[1]), (-A_I[0], A_I[1])]


def make_plate(sign):
    """sign=-1 front plate (-Y), +1 back plate (+Y)."""
    y0, y1 = (-OUT_HW, -GAP_HW) if sign < 0 else (GAP_HW, OUT_HW)
    pl = xz_solid(plate_profile, y0, y1)
    # round only the perimeter of the outer face
    pl = pl.faces("<Y" if sign < 0 else ">Y").edges().fillet(PLATE_EDGE_R)
    # workplane on the outer face, normal pointing outwards
    if sign < 0:
        wp = cq.Workplane("XZ", origin=(0, y0, 0))
    else:
        wp = cq.Workplane("XZ", origin=(0, y1, 0)).transformed(rotate=(0, 180, 0))

    def lx(x):
        return x if sign < 0 else -x

    piv = [(lx(x), z) for x, z in PIVOTS]
    scr = [(lx(x), z) for x, z in SCREWS]
    # pivot bores through the plate (the hollow pins end PIN_RECESS below the face)
    pl = pl.cut(wp.pushPoints(piv).circle(PIVOT_R).extrude(-PLATE_T))
    # socket head screws standing slightly proud of the plate, in a shallow counterbore
    pl = pl.cut(wp.pushPoints(scr).circle(SCREW_R + 0.5).extrude(-0.4))
    heads = wp.workplane(offset=-0.4).pushPoints(scr).circle(SCREW_R).extrude(SCREW_H + 0.4)
    heads = heads.faces("<Y" if sign < 0 else ">Y").edges().fillet(0.5)
    pl = pl.union(heads)
    pl = pl.cut(wp.workplane(offset=SCREW_H).pushPoints(scr).circle(1.4).extrude(-1.2))
    return pl


# ---- core box -----------------------------------------------------------------
def make_core():
    core = cq.Workplane("XY").box(2 * BODY_HW, 2 * GAP_HW, CORE_TOP, centered=(True, True, False))
    core = core.edges("|Y and >Z").fillet(CORE_TOP_R)
    core = core.edges("|Y and <Z").fillet(CORNER_R)
    # side wall small holes
    pts = [(-11.5, 10.2), (11.5, 10.2), (-11.5, 82.0), (11.5, 82.0)]
    for sx in (-1, 1):
        cutter = cq.Workplane("YZ", origin=(sx * (BODY_HW + 1.0), 0, 0)).pushPoints(pts) \
            .circle(SIDE_HOLE_R).extrude(-sx * 5.0)
        core = core.cut(cutter)
    # larger port on the left wall
    port = cq.Workplane("YZ", origin=(-BODY_HW - 1.0, 0, 0)).center(0, 33.0).circle(4.0).extrude(7.0)
    core = core.cut(port)
    # bottom: central recess + 4 holes
    core = core.cut(cq.Workplane("XY").circle(BOTTOM_REC_R).extrude(2.5))
    core = core.cut(cq.Workplane("XY").pushPoints(
        [(-20.7, -12.0), (20.7, -12.0), (-20.7, 12.0), (20.7, 12.0)]).circle(1.0).extrude(6.0))
    return core


# ---- linkage -------------------------------------------------------------------
LINK_LEN = math.hypot(*LINK_V)
LINK_ANG = math.degrees(math.atan2(-LINK_V[1], LINK_V[0]))  # rotation about +Y


def place_link(solid, a):
    """Link built along local +X from the origin; rotate onto the link axis."""
    return solid.rotate((0, 0, 0), (0, 1, 0), LINK_ANG).translate((a[0], 0, a[1]))


def pin_mark(x, y_face, s, r=2.3, depth=1.1):
    return cq.Workplane("XZ", origin=(0, y_face + s * 0.5, 0)).center(x, 0).circle(r) \
        .extrude((depth + 0.5) * s)


def make_outer_link():
    L = LINK_LEN
    body = cq.Workplane("XZ", origin=(0, OUTER_LINK_HW, 0)).center(L / 2, 0) \
        .slot2D(L + 2 * LINK_R, 2 * LINK_R).extrude(2 * OUTER_LINK_HW)
    # fork gap at the jaw end
    fork = cq.Workplane("XY").box(16.0, 2 * FORK_HW, 3 * LINK_R).translate((L + 1.0, 0, 0))
    body = body.cut(fork)
    # window pocket on the outer face (+Z local)
    pocket = cq.Workplane("XY").box(43.0, 2 * FORK_HW, POCKET_D).edges("|Z").fillet(2.0) \
        .translate((10.0 + 21.5, 0, LINK_R - POCKET_D / 2 + 0.001))
    body = body.cut(pocket)
    # through slot in the pocket floor
    slot = cq.Workplane("XY").box(SLOT_LEN, 4.6, 4 * LINK_R).edges("|Z").fillet(2.2) \
        .translate((SLOT_C, 0, 0))
    body = body.cut(slot)
    # pin end marks at the jaw end
    for s in (-1, 1):
        body = body.cut(pin_mark(L, s * OUTER_LINK_HW, s))
    return place_link(body, A_O)


def make_inner_links():
    """Wide inner link: forked at the jaw end, with a through slot."""
    L = LINK_LEN
    body = cq.Workplane("XZ", origin=(0, OUTER_LINK_HW, 0)).center(L / 2, 0) \
        .slot2D(L + 2 * LINK_R, 2 * LINK_R).extrude(2 * OUTER_LINK_HW)
    fork_t0 = L - INNER_FORK_L
    fork = cq.Workplane("XY").box(INNER_FORK_L + 10.0, 2 * FORK_HW, 3 * LINK_R) \
        .translate((fork_t0 + (INNER_FORK_L + 10.0) / 2, 0, 0))
    body = body.cut(fork)
    slot = cq.Workplane("XY").box(INNER_SLOT_LEN, 4.6, 4 * LINK_R).edges("|Z").fillet(2.2) \
        .translate((INNER_SLOT_C, 0, 0))
    body = body.cut(slot)
    # pin through at the jaw end (joins link to the jaw arm)
    pin = cq.Workplane("XZ", origin=(0, OUTER_LINK_HW - 0.6, 0)).center(L, 0).circle(2.3) \
        .extrude(2 * OUTER_LINK_HW - 1.2)
    body = body.union(pin)
    for s in (-1, 1):
        body = body.cut(pin_mark(L, s * OUTER_LINK_HW, s))
    return place_link(body, A_I)


def make_pins():
    """Pivot pins spanning both plates (left side), ends recessed in the bores.
    (Their through bore is cut at the end, through the whole stack.)"""
    res = None
    half = OUT_HW - PIN_RECESS
    for p in (A_O, A_I):
        pin = cq.Workplane("XZ", origin=(0, half, 0)).center(p[0], p[1]) \
            .circle(PIVOT_R).extrude(2 * half)
        res = pin if res is None else res.union(pin)
    return res


# ---- jaws -------------------------------------------------------------------------
def make_jaw():
    """Left jaw: gripping block on top, body with stem, arm and knuckle."""
    block = cq.Workplane("XY").box(JAW_HW - JAW_GAP, 2 * JAW_D_HW, JAW_Z1 - JAW_Z0) \
        .translate((-(JAW_HW + JAW_GAP) / 2, 0, (JAW_Z0 + JAW_Z1) / 2))
    block = block.edges("|Y and <X and >Z").fillet(JAW_TOP_R)
    block = block.edges("|Y and <X and <Z").fillet(1.5)
    kx, kz = B_O
    kr = KNUCKLE_R
    # lower edge: from the stem side, tangent to the underside of the knuckle
    px, pz = -STEM_HW, STEM_SIDE_Z
    dkx, dkz = kx - px, kz - pz
    dk = math.hypot(dkx, dkz)
    ang = math.atan2(dkz, dkx) + math.asin(kr / dk)
    lo = (math.cos(ang), math.sin(ang))
    # upper edge: line tangent to the top of the knuckle with slope ARM_SLOPE
    up = (1.0 / math.hypot(1.0, ARM_SLOPE), ARM_SLOPE / math.hypot(1.0, ARM_SLOPE))
    nrm = (-up[1], up[0])
    tx, tz = kx + kr * nrm[0], kz + kr * nrm[1]
    # intersection of both edge lines -> polygon vertex filleted with the knuckle radius
    # px + lo.x*t = tx + up.x*u ; pz + lo.z*t = tz + up.z*u
    det = lo[0] * (-up[1]) - lo[1] * (-up[0])
    t = ((tx - px) * (-up[1]) - (tz - pz) * (-up[0])) / det
    vx, vz = px + lo[0] * t, pz + lo[1] * t
    cx = -ARM_NECK_HW
    cz = tz + ARM_SLOPE * (cx - tx)
    jz = JAW_Z0 + 1.0
    pts = [(-JAW_GAP, STEM_Z0), (-STEM_HW, STEM_Z0), (px, pz), (vx, vz), (cx, cz),
           (cx, jz), (-JAW_GAP, jz)]
    radii = [0.0, 1.5, 1.0, kr, ARM_NECK_R, 0.0, 0.0]

    def prof(wp):
        return fillet_poly(wp, pts, radii)

    body = xz_solid(prof, -FORK_HW, FORK_HW)
    return block.union(body)


def jaw_teeth_cutter():
    """Vertical V-grooves along the jaw mating plane (serration)."""
    cut = None
    for i in range(TEETH_N):
        y = (i - (TEETH_N - 1) / 2.0) * TEETH_P
        d = cq.Workplane("XY").center(0, y).rect(TEETH_D, TEETH_D) \
            .extrude(JAW_Z1 - JAW_Z0 + 2) \
            .rotate((0, y, 0), (0, y, 1), 45).translate((0, 0, JAW_Z0 - 0.5))
        cut = d if cut is None else cut.union(d)
    return cut


def build_side():
    side = make_outer_link()
    for p in (make_inner_links(), make_pins(), make_jaw()):
        side = side.union(p)
    return side


left = build_side()
right = left.mirror("YZ")

housing = make_core().union(make_plate(-1)).union(make_plate(1))

# bores of the hollow pivot pins, through the whole stack
bores = cq.Workplane("XZ", origin=(0, OUT_HW + 1.0, 0)).pushPoints(PIVOTS) \
    .circle(PIN_BORE_R).extrude(2 * OUT_HW + 2.0)

result = housing.union(left).union(right).cut(jaw_teeth_cutter()).cut(bores)

VIEW = {"azimuth": 45, "elevation": 26}
